import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_X = 99.5           # plate width (X)
L_Y = 155.0          # plate length (Y)
T = 19.0             # plate thickness (Z)
CORNER_CH = 5.8      # 45 deg vertical corner chamfers

# rim widths around the pocket (the pocket sits slightly off-centre in X)
BORDER_XN = 15.45    # rim on the -X side
BORDER_XP = 13.8     # rim on the +X side
BORDER_Y = 14.75     # rim on the -Y / +Y sides
POCKET_D = 14.5     # pocket depth from top face

SLOT_W = 27.5        # slot width at the top (X)
SLOT_CX = -0.25      # slot centre X
SLOT_D = 11.0        # slot depth from top face
SLOT_CH_H = 4.5      # bottom chamfer, horizontal leg
SLOT_CH_V = 4.5      # bottom chamfer, vertical leg (45 deg)

HOLE_OFF = 7.35      # hole centre distance from the outer edges
HOLE_D = 5.0         # through hole diameter
CB_D = 9.0           # counterbore diameter (from underside)
CB_DEPTH = 5.0       # counterbore depth

# engraved label on the underside (readable from below)
LABEL_LINES = ["Mosaic", "Productivity", "board"]
LABEL_SIZE = 5.5     # font size
LABEL_PITCH = 7.2    # line pitch
LABEL_X = -2.0       # label centre X
LABEL_Y = -47.0      # label centre Y
LABEL_DEPTH = 0.6    # engraving depth

# ---------------- base plate with chamfered corners ----------------
plate = (
    cq.Workplane("XY")
    .rect(L_X, L_Y)
    .extrude(T)
    .edges("|Z")
    .chamfer(CORNER_CH)
)

# ---------------- central pocket ----------------
pocket_w = L_X - BORDER_XN - BORDER_XP
pocket_l = L_Y - 2 * BORDER_Y
pocket_cx = (BORDER_XN - BORDER_XP) / 2.0
pocket = (
    cq.Workplane("XY", origin=(pocket_cx, 0, T - POCKET_D))
    .rect(pocket_w, pocket_l)
    .extrude(POCKET_D + 1.0)
)
plate = plate.cut(pocket)

# ---------------- cable slot through the +Y rim ----------------
zt = T + 1.0
zb = T - SLOT_D
zc = zb + SLOT_CH_V
hw = SLOT_W / 2.0
slot_pts = [
    (SLOT_CX - hw, zt),
    (SLOT_CX - hw, zc),
    (SLOT_CX - hw + SLOT_CH_H, zb),
    (SLOT_CX + hw - SLOT_CH_H, zb),
    (SLOT_CX + hw, zc),
    (SLOT_CX + hw, zt),
]
y_in = L_Y / 2.0 - BORDER_Y - 1.0
y_len = BORDER_Y + 2.0
# XZ workplane normal is -Y, so extrude negative to go toward +Y
slot = (
    cq.Workplane("XZ", origin=(0, y_in, 0))
    .polyline(slot_pts)
    .close()
    .extrude(-y_len)
)
plate = plate.cut(slot)

# ---------------- corner holes with underside counterbores ----------------
hx = L_X / 2.0 - HOLE_OFF
hy = L_Y / 2.0 - HOLE_OFF
hole_pts = [(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)]

holes = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .pushPoints(hole_pts)
    .circle(HOLE_D / 2.0)
    .extrude(T + 2.0)
)
cbores = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .pushPoints(hole_pts)
    .circle(CB_D / 2.0)
    .extrude(CB_DEPTH + 1.0)
)
plate = plate.cut(holes).cut(cbores)

# ---------------- engraved label on the underside ----------------
# workplane on the bottom face, normal pointing down (-Z), text baseline
# along +X so it reads correctly when the part is viewed from below.
# Wrapped so that a missing font can never break the main part.
try:
    labels = None
    n = len(LABEL_LINES)
    for i, line in enumerate(LABEL_LINES):
        off = (n - 1) / 2.0 * LABEL_PITCH - i * LABEL_PITCH
        pl = cq.Plane(
            origin=(LABEL_X, LABEL_Y - off, 0.0),
            xDir=(1, 0, 0),
            normal=(0, 0, -1),
        )
        txt = cq.Workplane(pl).text(
            line, LABEL_SIZE, -LABEL_DEPTH, combine=False,
            halign="center", valign="center",
        )
        labels = txt if labels is None else labels.union(txt)
    if labels is not None:
        engraved = plate.cut(labels)
        if engraved.val().isValid() and len(engraved.solids().vals()) == 1:
            plate = engraved
except Exception:
    pass

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
